import math
import cadquery as cq

# =====================================================================================
#  Fixture block with a V-jaw in front and two curved (twisted) blades at the back.
#  X to the right, Y to the back, Z up; origin at the top-left-front corner line of the
#  rear band (x=0 at its top-left edge, y=0 at its front face, z=0 at the common floor).
# =====================================================================================

# ---------------------------------------------------------------- main dimensions (mm)
H_TALL = 44.5          # height of the rear (bladed) body
H_LOW = 24.2           # height of the front block and V-jaw
X_RIGHT = 84.8         # common right face of band and block
BAND_D = 12.3          # depth (Y) of the solid band behind the block
Y_BACK = 60.35         # rear end of the blades

# ---------------------------------------------------------------- front block
BLK_X0 = 12.1          # left face of the block
BLK_Y0 = -52.8         # front face of the block

# ---------------------------------------------------------------- V-jaw (two 12 mm bars at 60 deg)
APEX = (32.8, -2.85)   # outer corner of the V
BISECT = -34.86        # direction of the V bisector (deg from +X)
HALF = 30.0            # half opening angle of the V
BAR_W = 12.0           # bar width
BAR_L = 60.5           # length of the outer edge of each bar
END_R = 12.0           # quarter-round at the bar ends
FIL_R = 8.4            # fillet in the inner corner of the V
APEX_R = 6.0           # circular relief at the apex
JAW_LIFT = 0.1         # the jaw body sits this much higher than the block (top and bottom)

# ---------------------------------------------------------------- blade faces
# Each curved face is described at its front and back end by (x at top, x at floor, sagitta of
# the circular section, bowing towards -X), plus a plan-view bow of its top and bottom edges.
#   F0 outer face of the left wall (starts at the front of the band, y = 0)
#   F1 inner face of the left wall, F2 left face of the middle rib, F3 right face of the middle rib
#   (these start at the back face of the band, y = BAND_D)
FACES = {
    #        front (top, floor, sag)  back (top, floor, sag)   bow top, bow floor
    "F0": ((0.0, 17.8, 3.3), (13.25, 40.6, 6.9), 0.8, 2.3),
    "F1": ((9.2, 24.7, 3.3), (18.85, 38.0, 3.9), 0.7, 0.5),
    "F2": ((21.9, 40.7, 3.3), (31.7, 55.8, 5.0), 0.6, 0.8),
    "F3": ((33.55, 49.1, 3.3), (43.3, 61.74, 3.0), 0.5, 1.0),
}


def face_section(name, y):
    """(x_top, x_floor, sagitta) of a blade face at depth y (quadratic bow in plan)."""
    fr, bk, bt, bb = FACES[name]
    y0 = 0.0 if name == "F0" else BAND_D
    t = (y - y0) / (Y_BACK - y0)
    b = 4.0 * t * (1.0 - t)
    xt = fr[0] + (bk[0] - fr[0]) * t - bt * b
    xb = fr[1] + (bk[1] - fr[1]) * t - bb * b
    sg = fr[2] + (bk[2] - fr[2]) * t
    return xt, xb, sg


def arc_pts(sec):
    """top, middle and floor point of a face section (arc bowing outwards, to -X)."""
    xt, xb, s = sec
    p0, p1 = (xt, H_TALL), (xb, 0.0)
    mx, mz = (p0[0] + p1[0]) / 2, (p0[1] + p1[1]) / 2
    cx, cz = p1[0] - p0[0], p1[1] - p0[1]
    ln = math.hypot(cx, cz)
    nx, nz = cz / ln, -cx / ln
    if nx > 0:
        nx, nz = -nx, -nz
    return p0, (mx + s * nx, mz + s * nz), p1


def xz_wire(seq, y):
    """closed wire in the plane Y=y from [('S', p), ('L', p) | ('A', pmid, p), ...] (XZ coords)."""
    V = lambda p: cq.Vector(p[0], y, p[1])
    edges, cur = [], seq[0][1]
    start = cur
    for item in seq[1:]:
        if item[0] == "L":
            edges.append(cq.Edge.makeLine(V(cur), V(item[1])))
            cur = item[1]
        else:
            edges.append(cq.Edge.makeThreePointArc(V(cur), V(item[1]), V(item[2])))
            cur = item[2]
    if math.hypot(cur[0] - start[0], cur[1] - start[1]) > 1e-9:
        edges.append(cq.Edge.makeLine(V(cur), V(start)))
    return cq.Wire.assembleEdges(edges)


EXT = 6.0  # cutters overshoot the body above and below


def body_wire(y):
    p0, pm, p1 = arc_pts(face_section("F0", y))
    return xz_wire([("S", p0), ("A", pm, p1), ("L", (X_RIGHT, 0.0)), ("L", (X_RIGHT, H_TALL))], y)


def slot_wire(y):
    a0, am, a1 = arc_pts(face_section("F1", y))
    b0, bm, b1 = arc_pts(face_section("F2", y))
    return xz_wire([("S", a0), ("A", am, a1), ("L", (a1[0], -EXT)), ("L", (b1[0], -EXT)), ("L", b1),
                    ("A", bm, b0), ("L", (b0[0], H_TALL + EXT)), ("L", (a0[0], H_TALL + EXT))], y)


def right_wire(y, xr=140.0):
    a0, am, a1 = arc_pts(face_section("F3", y))
    return xz_wire([("S", a0), ("A", am, a1), ("L", (a1[0], -EXT)), ("L", (xr, -EXT)),
                    ("L", (xr, H_TALL + EXT)), ("L", (a0[0], H_TALL + EXT))], y)


def loft(wires):
    return cq.Workplane("XY").add(cq.Solid.makeLoft(wires, False))


# ---------------------------------------------------------------- rear body: band + two curved blades
body = loft([body_wire(y) for y in (0.0, Y_BACK / 2, Y_BACK)])
ys_cut = (BAND_D, (BAND_D + Y_BACK) / 2, Y_BACK + 4.0)
slot_cut = loft([slot_wire(y) for y in ys_cut])
right_cut = loft([right_wire(y) for y in ys_cut])
rear = body.cut(slot_cut).cut(right_cut)


# ---------------------------------------------------------------- V-jaw outline
def rot(p, ang):
    c, s = math.cos(ang), math.sin(ang)
    return (p[0] * c - p[1] * s, p[0] * s + p[1] * c)


def jaw_points():
    """key points of the jaw outline in a local frame (apex at origin, bisector along +x)."""
    h = math.radians(HALF)
    e1, e2 = (math.cos(h), math.sin(h)), (math.cos(h), -math.sin(h))
    n1, n2 = (math.sin(h), -math.cos(h)), (math.sin(h), math.cos(h))   # inward normals
    L0 = BAR_L - END_R
    k = 1.0 / math.sqrt(2.0)

    def P(a, e, b, n):
        return (a * e[0] + b * n[0], a * e[1] + b * n[1])

    q1, q2 = P(L0, e1, 0, n1), P(L0, e2, 0, n2)
    cdist = BAR_W / math.sin(h)             # inner corner on the bisector
    t = FIL_R / math.tan(h)
    pts = {
        "a1": P(APEX_R, e1, 0, n1),
        "o1": P(BAR_L, e1, 0, n1),
        "m1": (q1[0] + END_R * k * (e1[0] + n1[0]), q1[1] + END_R * k * (e1[1] + n1[1])),
        "i1": P(L0, e1, BAR_W, n1),
        "t1": (cdist + t * e1[0], t * e1[1]),
        "fm": (cdist + FIL_R / math.sin(h) - FIL_R, 0.0),
        "t2": (cdist + t * e2[0], t * e2[1]),
        "i2": P(L0, e2, BAR_W, n2),
        "m2": (q2[0] + END_R * k * (e2[0] + n2[0]), q2[1] + END_R * k * (e2[1] + n2[1])),
        "o2": P(BAR_L, e2, 0, n2),
        "a2": P(APEX_R, e2, 0, n2),
        "am": (APEX_R, 0.0),
    }
    ang = math.radians(BISECT)
    return {k2: (APEX[0] + rot(v, ang)[0], APEX[1] + rot(v, ang)[1]) for k2, v in pts.items()}


J = jaw_points()


def jaw_sketch():
    return (cq.Workplane("XY")
            .moveTo(*J["a1"]).lineTo(*J["o1"])
            .threePointArc(J["m1"], J["i1"])
            .lineTo(*J["t1"])
            .threePointArc(J["fm"], J["t2"])
            .lineTo(*J["i2"])
            .threePointArc(J["m2"], J["o2"])
            .lineTo(*J["a2"])
            .threePointArc(J["am"], J["a1"])
            .close())


jaw = jaw_sketch().extrude(H_LOW).translate((0, 0, JAW_LIFT))

# ---------------------------------------------------------------- block: rectangle minus the V opening
blk = cq.Workplane("XY").box(X_RIGHT - BLK_X0, -BLK_Y0, H_LOW, centered=False).translate((BLK_X0, BLK_Y0, 0))
ang, h, far = math.radians(BISECT), math.radians(HALF), 200.0
w1 = rot((far * math.cos(h), far * math.sin(h)), ang)
w2 = rot((far * math.cos(h), -far * math.sin(h)), ang)
wedge = (cq.Workplane("XY").moveTo(*APEX).lineTo(APEX[0] + w1[0], APEX[1] + w1[1])
         .lineTo(APEX[0] + w2[0], APEX[1] + w2[1]).close().extrude(H_LOW))
apex_disc = cq.Workplane("XY").center(*APEX).circle(APEX_R).extrude(H_LOW)
jaw_region = jaw_sketch().extrude(H_LOW)
blk = blk.cut(wedge.cut(apex_disc).cut(jaw_region))      # only the opening between the bars is removed

result = rear.union(blk).union(jaw)

VIEW = {"azimuth": 45, "elevation": 26}
